import math
import cadquery as cq

# ---------------------------------------------------------------
# Kit of parts laid out flat (one compound of separate solids):
#  - two finger-jointed plates with complementary fingers,
#  - two mold boxes built from wall panels, each holding a mirror-
#    handed domed pattern (ball socket, two jaws, sprue ridge),
#  - two square posts, four hex nuts, two pinned cam discs with hex
#    sockets, a lever rod with a cross hole and a ball knob, and two
#    tall hex bars.
# All driving dimensions in mm (multiples of a base unit U).
# ---------------------------------------------------------------
U = 2.0  # base unit (mm)

# ---- plates ----------------------------------------------------
PL_L = 82.4 * U      # length incl. finger tabs (X)
PL_W = 34.4 * U      # width (Y)
PL_T = 3.7 * U       # thickness
N_FING = 13          # tab/notch segments along each short edge (tabs at corners)
SQ_HOLE = 2.5 * U    # small square hole
RD_HOLE = 3.4 * U    # round hole dia
SLOT_X, SLOT_Y = 5.0 * U, 3.5 * U
SQ_HOLE_POS = (-8.7 * U, 2.1 * U)        # relative to plate centre
RD_HOLE_POS = (3.0 * U, -1.4 * U)
SLOT_POS = [(-8.9 * U, -13.0 * U), (13.8 * U, -13.0 * U)]
PLATE_GAP = 7.8 * U
PLATE2_XOFF = 0.7 * U  # back plate shifted slightly in +X

# ---- boxes -----------------------------------------------------
BX_W = 29.3 * U      # X
BX_D = 43.2 * U      # Y
BX_H = 17.9 * U      # Z
BX_T = 2.1 * U       # wall thickness
BX_F = 2.5 * U       # floor thickness
BX_Z0 = 1.8 * U      # boxes sit slightly raised
BOX1_C = (109.55 * U, 23.2 * U)
BOX2_C = (143.4 * U, 23.2 * U)
MARK_DX, MARK_DY = 10.1 * U, 15.4 * U   # corner alignment pins / holes
MARK_D = 1.2 * U
# domed pattern inside each box (box-1 handed; box 2 is mirrored)
DOME_AX, DOME_AY = 9.2 * U, 15.0 * U   # footprint oval semi-axes
DOME_EY = 1.2 * U     # footprint centre (toward the prongs)
DOME_ZT = 12.8 * U    # parting face height at the socket
DOME_SOCK = (-1.4 * U, 0.6 * U)   # ball socket centre
DOME_AZ = 16.6 * U
DOME_TAN = 0.36       # slope of the parting face (down toward the prongs)
DOME_SLIT_Z = 3.0 * U
DOME_BALL_R = 3.9 * U
SPRUE_R = 1.1 * U

# ---- hardware --------------------------------------------------
POST_A = 3.6 * U
POST_H = 11.6 * U
POST_C = (170.9 * U, 26.2 * U)
POST_PITCH = 3.8 * U

NUT_AF = 3.3 * U
NUT_H = 1.4 * U
NUT_HOLE = 2.1 * U
NUT_C = (173.7 * U, 10.9 * U)
NUT_PX, NUT_PY = 5.0 * U, 4.0 * U

DISC_D = 11.8 * U
DISC_H = 2.2 * U
DISC_HEX = 3.0 * U
DISC1_C = (186.1 * U, 29.1 * U)
DISC2_C = (199.0 * U, 29.1 * U)
PIN1_D, PIN1_TOP, PIN1_OFF = 3.7 * U, 15.2 * U, 3.9 * U
PIN2_D, PIN2_TOP, PIN2_OFF = 2.2 * U, 6.3 * U, 4.4 * U

ROD_D = 4.2 * U
ROD_X0 = 184.0 * U
BALL_D = 9.1 * U
BALL_C = (232.4 * U, 12.7 * U, 5.4 * U)
ROD_HOLE_X = 205.3 * U
ROD_HOLE_D = 3.0 * U

BAR_AC = 3.6 * U      # hex bar across corners
BAR_CH = 0.35 * U     # top chamfer
BAR1_H = 41.0 * U
BAR2_H = 41.8 * U
BAR1_C = (212.8 * U, 25.5 * U)
BAR2_C = (217.3 * U, 25.5 * U)


# ================================================================
def make_plate(corner_tabs_left):
    """Finger-jointed plate.  One short end has tabs at both corners, the
    opposite end has notches at both corners (complementary fingers)."""
    p = cq.Workplane("XY").box(PL_L, PL_W, PL_T, centered=(True, True, False))
    seg = PL_W / N_FING
    for end in (-1, 1):
        xe = end * (PL_L / 2 - PL_T / 2)
        tabs_at_corners = corner_tabs_left if end < 0 else not corner_tabs_left
        first = 1 if tabs_at_corners else 0
        for i in range(first, N_FING, 2):
            yc = -PL_W / 2 + seg * (i + 0.5)
            w = seg + (0.02 if i in (0, N_FING - 1) else 0.0)
            yo = -0.01 if i == 0 else (0.01 if i == N_FING - 1 else 0.0)
            cut = (cq.Workplane("XY")
                   .box(PL_T + 0.02, w, PL_T + 2, centered=(True, True, False))
                   .translate((xe + end * 0.01, yc + yo, -1)))
            p = p.cut(cut)
    # holes
    p = (p.faces(">Z").workplane(centerOption="CenterOfBoundBox")
         .pushPoints([SQ_HOLE_POS]).rect(SQ_HOLE, SQ_HOLE).cutThruAll())
    p = (p.faces(">Z").workplane(centerOption="CenterOfBoundBox")
         .pushPoints([RD_HOLE_POS]).hole(RD_HOLE))
    p = (p.faces(">Z").workplane(centerOption="CenterOfBoundBox")
         .pushPoints(SLOT_POS)
         .rect(SLOT_X, SLOT_Y).cutThruAll())
    return p.val()


def ellipsoid(ax, ay, az):
    s = cq.Solid.makeSphere(1.0, angleDegrees1=-90, angleDegrees2=90)
    m = cq.Matrix([[ax, 0, 0, 0], [0, ay, 0, 0], [0, 0, az, 0]])
    return s.transformGeometry(m)


def make_mold_insert(mirror):
    """Domed pattern on the floor of a mold box (local coords, floor at z=0)."""
    ztop = DOME_ZT
    sx, sy = DOME_SOCK
    # mound: ellipsoidal flanks, top sliced by a face sloping toward the prongs
    e = ellipsoid(DOME_AX, DOME_AY, DOME_AZ).translate(cq.Vector(0, DOME_EY, 0))
    slope = math.degrees(math.atan(DOME_TAN))
    cutter = (cq.Workplane("XY").rect(60 * U, 60 * U).extrude(30 * U)
              .rotate((0, 0, 0), (1, 0, 0), -slope)
              .translate((sx, sy, ztop)))
    d = e.cut(cutter.val())
    # footprint: straight outer flank, two prong tips, slanted inner flank
    u = U
    fp = (cq.Workplane("XY")
          .moveTo(-8.7 * u, -20 * u)
          .lineTo(-8.7 * u, 3.0 * u)
          .lineTo(-7.2 * u, 13.0 * u)
          .threePointArc((-6.1 * u, 14.3 * u), (-4.9 * u, 13.5 * u))
          .lineTo(-3.1 * u, 15.3 * u)
          .threePointArc((-2.0 * u, 16.1 * u), (-0.9 * u, 15.4 * u))
          .lineTo(8.9 * u, -3.7 * u)
          .lineTo(8.9 * u, -20 * u)
          .close()
          .extrude(ztop + 10 * u).translate((0, 0, -1)))
    d = d.intersect(fp.val())
    # V slit between the two prongs
    slit = (cq.Workplane("XY")
            .polyline([(-2.2 * u, 2.5 * u), (-5.0 * u, 17 * u), (-2.9 * u, 17 * u),
                      (-0.6 * u, 2.5 * u)]).close()
            .extrude(ztop + 10 * u).translate((0, 0, DOME_SLIT_Z)))
    d = d.cut(slit.val())
    # ball socket cavity (centre on the parting face)
    ball = cq.Solid.makeSphere(DOME_BALL_R, cq.Vector(sx, sy, ztop), cq.Vector(0, 0, 1),
                               -90, 90, 360)
    d = d.cut(ball)
    # sprue ridge running to the front wall
    ridge_len = BX_D / 2 - BX_T - 9.5 * u
    ridge = (cq.Workplane("XZ").circle(SPRUE_R).extrude(ridge_len)
             .translate((sx, -9.5 * u, 0)))
    d = d.fuse(ridge.val())
    # keep above floor
    d = d.intersect(cq.Solid.makeBox(40 * U, 40 * U, ztop + 10 * U,
                                     pnt=cq.Vector(-20 * U, -20 * U, 0)))
    if mirror:
        d = d.mirror("YZ")
    return d


def make_box(cx, cy, mirror):
    z0 = BX_Z0
    parts = []
    # side walls (full depth)
    for s in (-1, 1):
        w = cq.Solid.makeBox(BX_T, BX_D, BX_H,
                             pnt=cq.Vector(cx + s * (BX_W / 2 - BX_T / 2) - BX_T / 2,
                                           cy - BX_D / 2, z0))
        parts.append(w)
    # end walls (between side walls)
    for s in (-1, 1):
        w = cq.Solid.makeBox(BX_W - 2 * BX_T, BX_T, BX_H,
                             pnt=cq.Vector(cx - BX_W / 2 + BX_T,
                                           cy + s * (BX_D / 2 - BX_T / 2) - BX_T / 2, z0))
        parts.append(w)
    # floor with pattern
    floor = cq.Solid.makeBox(BX_W - 2 * BX_T, BX_D - 2 * BX_T, BX_F,
                             pnt=cq.Vector(cx - BX_W / 2 + BX_T, cy - BX_D / 2 + BX_T, z0))
    ins = make_mold_insert(mirror).translate(cq.Vector(cx, cy, z0 + BX_F))
    floor = floor.fuse(ins)
    # alignment marks in the corners
    for dx in (-MARK_DX, MARK_DX):
        for dy in (-MARK_DY, MARK_DY):
            c = cq.Solid.makeCylinder(MARK_D / 2, 1.0 * U,
                                      cq.Vector(cx + dx, cy + dy, z0 + BX_F))
            if mirror:
                floor = floor.cut(c.translate(cq.Vector(0, 0, -0.5 * U)))
            else:
                floor = floor.fuse(c)
    parts.append(floor.clean())
    return parts


def hex_prism(af, h, rot=0.0):
    ac = af / math.cos(math.radians(30))
    return (cq.Workplane("XY").polygon(6, ac).extrude(h)
            .rotate((0, 0, 0), (0, 0, 1), rot))


def make_nut():
    n = hex_prism(NUT_AF, NUT_H, 0).faces(">Z").workplane().hole(NUT_HOLE)
    return n.val()


def make_disc(pins):
    d = (cq.Workplane("XY").circle(DISC_D / 2).extrude(DISC_H)
         .cut(hex_prism(DISC_HEX, DISC_H + 2, 45).translate((0, 0, -1))))
    for (px, py, dia, top) in pins:
        d = d.union(cq.Workplane("XY").center(px, py).circle(dia / 2).extrude(top))
    return d.val()


def make_rod():
    """Lever rod with a cross hole, and the ball knob pressed onto its end."""
    bx, by, bz = BALL_C
    # ball: parametric seam placed on the rod side (-X) so it stays hidden
    ball = cq.Solid.makeSphere(BALL_D / 2, cq.Vector(bx, by, bz), cq.Vector(0, 0, -1),
                               -90, 90, 360)
    rod = (cq.Workplane("YZ").circle(ROD_D / 2).extrude(bx - ROD_X0)
           .translate((ROD_X0, by, bz)))
    hole = (cq.Workplane("XY").circle(ROD_HOLE_D / 2).extrude(ROD_D * 2)
            .translate((ROD_HOLE_X, by, bz - ROD_D)))
    rod = rod.cut(hole).val().cut(ball)
    return [rod, ball]


# ================================================================
solids = []

# front plate: notches at the corners on its -X end; back plate: tabs there
solids.append(make_plate(False).translate(cq.Vector(PL_L / 2, PL_W / 2, 0)))
solids.append(make_plate(True).translate(cq.Vector(PL_L / 2 + PLATE2_XOFF,
                                                   PL_W / 2 + PL_W + PLATE_GAP, 0)))

solids += make_box(BOX1_C[0], BOX1_C[1], False)
solids += make_box(BOX2_C[0], BOX2_C[1], True)

for k in range(2):
    solids.append(cq.Solid.makeBox(POST_A, POST_A, POST_H,
                                   pnt=cq.Vector(POST_C[0] - POST_A / 2,
                                                 POST_C[1] - POST_A / 2 + (k - 0.5) * POST_PITCH,
                                                 0)))

nut = make_nut()
for i in (-0.5, 0.5):
    for j in (-0.5, 0.5):
        solids.append(nut.translate(cq.Vector(NUT_C[0] + i * NUT_PX, NUT_C[1] + j * NUT_PY, 0)))

disc1 = make_disc([(0, PIN1_OFF, PIN1_D, PIN1_TOP)])
disc2 = make_disc([(0, PIN2_OFF, PIN2_D, PIN2_TOP), (0, -PIN2_OFF, PIN2_D, PIN2_TOP)])
solids.append(disc1.translate(cq.Vector(DISC1_C[0], DISC1_C[1], 0)))
solids.append(disc2.translate(cq.Vector(DISC2_C[0], DISC2_C[1], 0)))

solids += make_rod()

af_bar = BAR_AC * math.cos(math.radians(30))
for (bc, bh, rot) in ((BAR1_C, BAR1_H, 15), (BAR2_C, BAR2_H, 0)):
    bar = hex_prism(af_bar, bh, rot).faces(">Z").edges().chamfer(BAR_CH)
    solids.append(bar.translate((bc[0], bc[1], 0)).val())

result = cq.Compound.makeCompound(solids)

VIEW = {"azimuth": 45, "elevation": 26}
